import math
import cadquery as cq

# =====================================================================
#  Slanted display bezel / stand with side knob boss and a loose plug
#  X = width (part centred on X=0), Y = depth (front face at Y=0),
#  Z = height (bottom at Z=0).  The slanted face is at the back (+Y).
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
W = 167.5          # overall width (X)
H = 100.0          # overall height (Z)
T_LIP = 3.7        # thickness of the front bezel lip (Y)
D_TOP = 10.3       # depth at the top (incl. lip)
D_BOT = 37.0       # depth at the bottom (incl. lip)

LIP_L = 6.8        # left leg width of the front lip
LIP_R = 7.7        # right leg width of the front lip
LIP_TOP = 7.2      # top strip height of the front lip
LIP_BOT_Z = 10.7   # lower end of the lip legs (lip is an inverted U)

WALL = 2.7         # side wall thickness
FLOOR = 2.9        # floor thickness
TOP_WALL = 2.7     # top wall thickness
T_BACK = 3.0       # slanted back plate thickness (normal to plate)

# window in the slanted back plate (X measured from the left edge,
# Z heights measured on the outer slanted face)
WIN_X0 = 14.0
WIN_X1 = 144.8
WIN_Z0 = 12.9
WIN_Z1 = 90.5
WIN_CH = 1.3       # 45 deg bevel around the window on the slanted face

# side boss on the right wall
BOSS_D = 12.8      # protrusion in +X
BOSS_RT = 13.5     # vertical extent of the upper rounding
BOSS_RB = 9.0      # vertical extent of the lower rounding
BOSS_ZT = 71.6     # top of boss (horizontal)
BOSS_ZB = 19.3     # bottom of boss at the front face
BOSS_SLOPE = 0.26  # rise of the boss bottom toward the back (dz/dy)

# circular knob recess on the slanted face
REC_X = 79.0       # centre X
REC_Z = 49.3       # centre height (on the outer slanted face)
REC_R = 13.8       # recess radius
REC_DEPTH = 7.5    # recess depth from the slanted face
CUP_R = 14.8       # outer radius of the cup behind the recess
CUP_L = 6.0        # cup protrusion beyond the inner face of the plate
PIN_R = 2.5        # centre hole in the recess floor
REC_CH = 1.0       # 45 deg chamfer on the recess rim

# small rectangular port with a flange pocket on the inner face
PORT_X = 71.5
PORT_Z = 24.0
PORT_W = 9.5
PORT_H = 6.8
POCK_X = 70.2
POCK_Z = 23.2
POCK_W = 12.8
POCK_H = 12.0
POCK_D = 1.0

# loose plug for the port (shown exploded to the right)
PLUG_DX = 59.0     # shift in +X from its seat
PLUG_DN = 2.7      # pulled out of the seat along the plate normal
PLUG_FW = 12.0     # flange
PLUG_FH = 9.6
PLUG_FT = 1.0
PLUG_SW = 8.6      # stem (elliptic section)
PLUG_SH = 6.0
PLUG_SL = 6.5
PLUG_SR = 1.2      # rounding of the stem end

# engraved logo on the underside
LOGO_DEPTH = 0.5
LOGO_SIZE = 19.0
LOGO_BASE_Y = 12.6                       # baseline position (Y)
LOGO_CHARS = [("P", 58.5), ("i", 44.3), ("o", 31.3), ("n", 15.1), ("e", -1.2),
              ("e", -16.8), ("r", -29.0), ("D", -51.2), ("J", -63.8)]

# ---------------- derived geometry ----------------
SLOPE = (D_BOT - D_TOP) / H              # dy/dz of the slanted face
ALPHA = math.atan(SLOPE)                 # tilt from vertical
CA, SA = math.cos(ALPHA), math.sin(ALPHA)


def y_out(z):
    return D_BOT - SLOPE * z


def y_in(z):
    return y_out(z) - T_BACK / CA


# plane on the outer slanted face: x = X, y = up the slope, z = into the part
BACK_PLANE = cq.Plane(origin=(0, D_BOT, 0), xDir=(1, 0, 0), normal=(0, -CA, -SA))


def s_of(z):
    """distance up the slope for a height z on the outer slanted face"""
    return z / CA


def back_wp(offset=0.0):
    return cq.Workplane(BACK_PLANE).workplane(offset=offset)


def wedge(x0, width):
    return (
        cq.Workplane("YZ", origin=(x0, 0, 0))
        .polyline([(T_LIP, 0), (D_BOT, 0), (D_TOP, H), (T_LIP, H)])
        .close()
        .extrude(width)
    )


# ---------------- main wedge body (open-front shell) ----------------
body = wedge(-W / 2, W)

zc0, zc1 = FLOOR, H - TOP_WALL
cavity = (
    cq.Workplane("YZ", origin=(-W / 2 + WALL, 0, 0))
    .polyline([(T_LIP - 1.0, zc0), (y_in(zc0), zc0), (y_in(zc1), zc1), (T_LIP - 1.0, zc1)])
    .close()
    .extrude(W - 2 * WALL)
)
body = body.cut(cavity)


# ---------------- side boss (D section, bottom rising toward the back) ----------------
def d_profile(wp, zb, zt):
    """D-shaped boss section: straight wall side + one smooth outer spline"""
    x0 = W / 2 - 0.5
    x1 = W / 2 + BOSS_D
    ax = BOSS_D - 0.3
    ct = (x1 - ax, zt - BOSS_RT)       # centre of the upper elliptic corner
    cb = (x1 - ax, zb + BOSS_RB)       # centre of the lower elliptic corner
    pts, tans = [(x0, zt)], [(1.0, 0.0)]
    for a in (90, 60, 30, 0):
        t = math.radians(a)
        pts.append((ct[0] + ax * math.cos(t), ct[1] + BOSS_RT * math.sin(t)))
        tans.append((ax * math.sin(t), -BOSS_RT * math.cos(t)))
    for a in (0, -30, -60, -90):
        t = math.radians(a)
        pts.append((cb[0] + ax * math.cos(t), cb[1] + BOSS_RB * math.sin(t)))
        tans.append((ax * math.sin(t), -BOSS_RB * math.cos(t)))
    pts.append((x0, zb))
    tans.append((-1.0, 0.0))
    tans = [(tx / math.hypot(tx, tz), tz / math.hypot(tx, tz)) for tx, tz in tans]
    return wp.moveTo(x0, zt).spline(pts[1:], tangents=tans, includeCurrent=True).close()


y_back = D_BOT + 2.0
boss = d_profile(cq.Workplane("XZ", origin=(0, T_LIP, 0)), BOSS_ZB, BOSS_ZT)
boss = d_profile(
    boss.workplane(offset=-(y_back - T_LIP)),
    BOSS_ZB + BOSS_SLOPE * (y_back - T_LIP),
    BOSS_ZT,
)
boss = boss.loft(ruled=True)
boss = boss.intersect(wedge(-W, 2 * W + 60))      # trim to the slanted face
body = body.union(boss)

# ---------------- features of the slanted plate ----------------
# display window (cut normal to the plate)
win = (
    back_wp(-5)
    .center((WIN_X0 + WIN_X1) / 2 - W / 2, (s_of(WIN_Z0) + s_of(WIN_Z1)) / 2)
    .rect(WIN_X1 - WIN_X0, s_of(WIN_Z1) - s_of(WIN_Z0))
    .extrude(T_BACK + 10)
)
body = body.cut(win)
win_bevel = (
    back_wp(-0.5)
    .center((WIN_X0 + WIN_X1) / 2 - W / 2, (s_of(WIN_Z0) + s_of(WIN_Z1)) / 2)
    .rect(WIN_X1 - WIN_X0 + 2 * (WIN_CH + 0.5), s_of(WIN_Z1) - s_of(WIN_Z0) + 2 * (WIN_CH + 0.5))
    .extrude(WIN_CH + 0.5, taper=45)
)
body = body.cut(win_bevel)

# cup behind the knob recess (kept inside the body width)
cup = back_wp(0).center(REC_X, s_of(REC_Z)).circle(CUP_R).extrude(T_BACK + CUP_L)
cup = cup.intersect(
    cq.Workplane("XY").box(W, 3 * D_BOT, 2 * H, centered=(True, False, False)).translate((0, -D_BOT, -H / 2))
)
body = body.union(cup)

# knob recess + centre hole
rec = back_wp(-2).center(REC_X, s_of(REC_Z)).circle(REC_R).extrude(REC_DEPTH + 2)
body = body.cut(rec)
rec_ch = back_wp(-0.5).center(REC_X, s_of(REC_Z)).circle(REC_R + REC_CH + 0.5).extrude(REC_CH + 0.5, taper=45)
body = body.cut(rec_ch)
pin = back_wp(-2).center(REC_X, s_of(REC_Z)).circle(PIN_R).extrude(T_BACK + CUP_L + 2.5)
body = body.cut(pin)

# small rectangular port and the flange pocket on the inner face
port = back_wp(-2).center(PORT_X, s_of(PORT_Z)).rect(PORT_W, PORT_H).extrude(T_BACK + 4)
body = body.cut(port)
pocket = back_wp(T_BACK - POCK_D).center(POCK_X, s_of(POCK_Z)).rect(POCK_W, POCK_H).extrude(POCK_D + 3)
body = body.cut(pocket)

# ---------------- engraved logo on the underside ----------------
# reads correctly when the part is viewed from below
LOGO_PLANE_X = (-1, 0, 0)
for ch, xc in LOGO_CHARS:
    try:
        glyph = cq.Workplane(
            cq.Plane(origin=(xc, LOGO_BASE_Y, 0), xDir=LOGO_PLANE_X, normal=(0, 0, -1))
        ).text(ch, LOGO_SIZE, -LOGO_DEPTH, combine=False, halign="center", valign="bottom", kind="bold")
        if glyph.solids().size() > 0:
            body = body.cut(glyph)
    except Exception:
        pass  # lettering is decorative only

# ---------------- front bezel lip (inverted U frame) ----------------
lip = (
    cq.Workplane("XY")
    .box(W, T_LIP, H - LIP_BOT_Z, centered=(True, False, False))
    .translate((0, 0, LIP_BOT_Z))
)
lip_open = (
    cq.Workplane("XY")
    .box(W - LIP_L - LIP_R, T_LIP + 2, H - LIP_TOP - LIP_BOT_Z + 2, centered=(False, False, False))
    .translate((-W / 2 + LIP_L, -1, LIP_BOT_Z - 2))
)
lip = lip.cut(lip_open)
# fused without face merging so that its outline stays visible as a seam
body = body.union(lip, clean=False)

# ---------------- loose plug, shown beside the part ----------------
# built in the slanted-face frame (x along X, y up the slope, z into the part)
f0 = T_BACK - POCK_D + PLUG_DN
pcx, pcy = POCK_X + PLUG_DX, s_of(PORT_Z)
plug_flange = (
    cq.Workplane("XY", origin=(0, 0, f0))
    .center(pcx, pcy)
    .rect(PLUG_FW, PLUG_FH)
    .extrude(PLUG_FT)
    .edges("|Z")
    .fillet(0.6)
)
plug_stem = (
    cq.Workplane("XY", origin=(0, 0, f0 - PLUG_SL))
    .center(pcx, pcy)
    .ellipse(PLUG_SW / 2, PLUG_SH / 2, rotation_angle=180)  # seam on the far side
    .extrude(PLUG_SL + 0.01)
    .faces("<Z")
    .edges()
    .fillet(PLUG_SR)
)
plug = plug_flange.union(plug_stem)
plug = cq.Workplane("XY").add(plug.val().moved(BACK_PLANE.location))

result = body.union(plug, clean=False)
